import cadquery as cq

# =====================================================================
#  Mounting plate with offset rectangular window, raised collar on the
#  back around the window and four countersunk holes in blended bosses.
#  Plate lies in the XZ plane, front face at y = 0 (facing -Y), all
#  raised features on the back (+Y).
# =====================================================================

# ================= driving dimensions (mm) =================
W = 125.0          # plate width  (X)
H = 99.7           # plate height (Z)
T = 1.4            # plate thickness (Y); front face y=0, back face y=T
R_CORNER = 6.2     # plate corner radius

# rectangular window through the plate
WIN_W = 62.5
WIN_H = 29.0
WIN_R = 4.2
WIN_DX = -8.0      # window centre offset in X (towards -X)

# raised rectangular collar on the back around the window
COL_H = 6.85       # collar height above the back face
COL_SHIFT_X = -0.25  # collar centre relative to the window centre (X)
COL_GAP_X = 0.8    # end walls stand back from the window edge (ledge)
COL_WALL_X = 3.7   # end walls (left/right) thickness
COL_GAP_Z = 1.9    # long walls stand back from the window edge (ledge)
COL_WALL_Z = 1.75  # long walls (top/bottom) thickness
COL_OUT_R = 1.0    # plan corner radius of the collar outline
COL_IN_R = 2.5     # plan corner radius of the collar opening
COL_FOOT_FIL = 2.2     # blend between collar and plate
COL_TOP_IN_CHAMF = 0.4 # chamfer on the inner top edge

# mounting holes with bosses on the back, countersunk from the front
HOLE_DX = 43.75    # half spacing X
HOLE_DZ = 40.0     # half spacing Z
HOLE_D = 5.8
CSK_D = 11.8
CSK_ANGLE = 90.0
BOSS_D = 14.5      # boss diameter at its top
BOSS_H = COL_H     # boss height above the back face
BOSS_FOOT = (2.5, 3.5)  # elliptical foot blend: radial reach, height

VIEW = {"azimuth": 45, "elevation": 26}

# ================= derived =================
hole_pts = [(sx * HOLE_DX, sz * HOLE_DZ) for sx in (-1, 1) for sz in (-1, 1)]
Y_TOP = T + COL_H
EPS = 0.02
SINK = T / 2       # construction overlap of added bodies into the plate

cx = WIN_DX + COL_SHIFT_X                     # collar centre X
in_w = WIN_W + 2 * COL_GAP_X                  # collar opening
in_h = WIN_H + 2 * COL_GAP_Z
col_w = in_w + 2 * COL_WALL_X                 # collar outline
col_h = in_h + 2 * COL_WALL_Z


def box_sel(x0, x1, y0, y1, z0, z1):
    return cq.selectors.BoxSelector((x0, y0, z0), (x1, y1, z1))


def rrect_prism(w, h, r, y0, depth, x_c=0.0):
    """Rounded rectangle in the XZ plane centred at (x_c, 0), from y0 toward
    +Y over 'depth'. ("XZ" workplane: local x -> X, local y -> Z, normal -Y)"""
    return (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .center(x_c, 0)
        .rect(w, h)
        .extrude(-depth)
        .edges("|Y")
        .fillet(r)
    )


# ================= plate =================
body = rrect_prism(W, H, R_CORNER, 0.0, T)

# ================= collar block =================
collar = rrect_prism(col_w, col_h, COL_OUT_R, T - SINK, COL_H + SINK, cx)
body = body.union(collar)

# foot blend of the collar (edges lying in the back face around the collar)
cbox = (cx - col_w / 2 - 1, cx + col_w / 2 + 1, -col_h / 2 - 1, col_h / 2 + 1)
body = body.edges(box_sel(cbox[0], cbox[1], T - EPS, T + EPS, cbox[2], cbox[3])).fillet(COL_FOOT_FIL)

# collar opening (above the plate only) + chamfer on its top edge
body = body.cut(rrect_prism(in_w, in_h, COL_IN_R, T, COL_H + 2, cx))
ibox = (cx - in_w / 2 - 0.1, cx + in_w / 2 + 0.1, -in_h / 2 - 0.1, in_h / 2 + 0.1)
body = body.edges(box_sel(ibox[0], ibox[1], Y_TOP - EPS, Y_TOP + EPS, ibox[2], ibox[3])).chamfer(COL_TOP_IN_CHAMF)


# ================= bosses (revolved: cylinder with elliptical foot) =================
def make_boss(x, z):
    r = BOSS_D / 2
    a, b = BOSS_FOOT
    prof = (
        cq.Workplane("XY")               # local x = radial, local y = height
        .moveTo(0, -SINK)
        .lineTo(r + a, -SINK)
        .lineTo(r + a, 0)
        # quarter ellipse: tangent to the plate, tangent to the cylinder
        .ellipseArc(a, b, 180, 270, sense=-1, startAtCurrent=True)
        .lineTo(r, BOSS_H)
        .lineTo(0, BOSS_H)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))   # about local Y = global Y
    )
    return prof.translate((x, T, z))


for (x, z) in hole_pts:
    body = body.union(make_boss(x, z))

# ================= window through the plate =================
body = body.cut(rrect_prism(WIN_W, WIN_H, WIN_R, -1.0, T + 2.0, WIN_DX))

# ================= countersunk holes from the front face =================
# (the hole pattern is symmetric in X and Z, so the face workplane's
#  in-plane orientation does not matter)
body = (
    body.faces("<Y").workplane(centerOption="ProjectedOrigin", origin=(0, 0, 0))
    .pushPoints(hole_pts)
    .cskHole(HOLE_D, CSK_D, CSK_ANGLE)
)

result = body
